import math
import cadquery as cq

# ---------------------------------------------------------------
# Parametric bracket / carriage body.
# Design units "u" are converted to millimetres with K.
# X: width (left/right), Y: length (front = -Y), Z: height
# ---------------------------------------------------------------
K = 0.25  # mm per design unit

VIEW = {"azimuth": 45, "elevation": 26}

# overall
TOP_Z = 146.0          # height of the tall walls
BODY_Y1 = 160.5        # rear end

# floor / channel
FLOOR_T = 17.6         # floor thickness at the rear end
FLOOR_T_FRONT = 13.4   # floor thickness at the channel mouth (top face slopes)
FLOOR_HX = 43.7        # half width of the floor between ledges
FLOOR_Y1 = 143.7       # rear end of floor plate
CH_OUT = 32.0          # channel outer half width
CH_IN = 24.0           # channel inner half width
CH_TOP = 72.0          # channel wall top
CH_FRONT = -76.0       # channel front end
CH_R_TOP = 13.0        # front top corner radius of channel walls
CH_R_BOT = 12.0        # front bottom corner radius
CH_ROUND = 1.0         # small round on the outer edges of the channel lip
BRIDGE_Y1 = 10.0       # back of the front bridge

# ledges / walls
LEDGE_TOP = 72.0
WALL_IN = 60.6         # inner face of tall walls (|X|)
WALL_OUT = 70.2        # outer face of tall walls (|X|) at the top
DRAFT_IN = 2.9         # inward offset of the outer faces at the bottom
WALL_BOT = 59.8        # underside of wall overhang
LIP_Y0 = 154.0         # rear inward lip
LOWER_FACE = 52.5      # recessed lower face under the wall (|X|)
RIB_OUT = 60.1         # outer rib tip (|X|)
RIB_Z0, RIB_Z1 = 27.3, 36.2
IRIB_IN = 57.0         # inner rib on wall inner face
IRIB_Y0, IRIB_Z1 = 57.5, 85.8

# front steps next to the blocks
STEP1_Z, STEP1_Y1 = 92.4, 10.0
STEP2_Z, STEP2_Y1 = 85.6, 14.6

# front blocks with cross holes
BLK_OUT_R = 81.5
BLK_OUT_L = 82.0
BLK_Y1 = 62.0
BLK_BOT_R = 59.8
BLK_BOT_L = 79.3
XH_R = 10.3            # cross hole radius
XH_DEPTH = 18.0
XH_UP_R = (30.8, 90.6)     # (Y, Z) right block hole
XH_UP_L = (33.3, 100.7)    # (Y, Z) left block hole
XH_LO_R = (15.4, 43.4)     # (Y, Z) lower hole in right front body
XH_LO_DEPTH = 16.0

# lower front body
LF_Y1 = 43.2
LF_X_HI = 60.6         # outer face |X| for Z in [LF_Z, WALL_BOT]
LF_X_LO = 51.7         # outer face |X| below LF_Z
LF_Z = 27.4
# thickened wall piece under the left block
LW_X = 73.5
LW_CH = 3.5

# bosses with large Y bores
BOSS_X = 113.0
BOSS_Y0, BOSS_Y1 = 43.2, 79.0
BOSS_R = 17.8
BOSS_R_Z0, BOSS_R_Z1 = 0.0, 59.8
BOSS_R_HX, BOSS_R_HZ = 86.7, 34.1
BOSS_L_Z0, BOSS_L_Z1 = 27.2, 79.3
BOSS_L_HX, BOSS_L_HZ = -86.5, 53.4

# left lower base
LB_X = 83.5
LB_Z = 27.2
CSK_X, CSK_Z, CSK_R, CSK_R2, CSK_D = -67.8, 13.8, 4.9, 9.6, 3.0
CSK_CH = 1.5           # chamfer at the rim of the counterbore
SLOT_Y0 = FLOOR_Y1     # rear slot from the screw hole inward

# floor holes
FH_R = 12.0
FH_YS = (71.6, 32.6, -4.8, -40.6)   # floor hole positions along Y
SH_R = 3.75
SH_X, SH_Y = 29.5, 124.4


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box((x1 - x0) * K, (y1 - y0) * K, (z1 - z0) * K, centered=False)
            .translate((x0 * K, y0 * K, z0 * K)))


def prism_xz(pts, y0, y1):
    """Polygon given in (x, z) design units, extruded along +Y from y0 to y1."""
    wp = cq.Workplane("XZ", origin=(0, y0 * K, 0))
    return wp.polyline([(x * K, z * K) for x, z in pts]).close().extrude(-(y1 - y0) * K)


def cyl_y(x, z, r, y0, y1):
    return (cq.Workplane("XZ", origin=(0, y0 * K, 0))
            .center(x * K, z * K).circle(r * K).extrude(-(y1 - y0) * K))


def cyl_x(y, z, r, x0, x1):
    # seam of the cylindrical face placed at the bottom of the bore
    pl = cq.Plane(origin=(x0 * K, y * K, z * K), xDir=(0, 0, -1), normal=(1, 0, 0))
    return cq.Workplane(pl).circle(r * K).extrude((x1 - x0) * K)


def cyl_z(x, y, r, z0, z1):
    return (cq.Workplane("XY", origin=(0, 0, z0 * K))
            .center(x * K, y * K).circle(r * K).extrude((z1 - z0) * K))


def floor_z(y):
    """Height of the (slightly inclined) floor top at position y."""
    return FLOOR_T_FRONT + (y - CH_FRONT) * (FLOOR_T - FLOOR_T_FRONT) / (FLOOR_Y1 - CH_FRONT)


def floor_prism(x0, x1, y0, y1):
    """Solid between the inclined floor top and z = TOP_Z + 10, spanning x0..x1."""
    pts = [(y0, floor_z(y0)), (y1, floor_z(y1)), (y1, TOP_Z + 10), (y0, TOP_Z + 10)]
    wp = cq.Workplane("YZ", origin=(x0 * K, 0, 0))
    return wp.polyline([(y * K, z * K) for y, z in pts]).close().extrude((x1 - x0) * K)


def floor_slab(x0, x1, y0, y1):
    pts = [(y0, 0), (y1, 0), (y1, floor_z(y1)), (y0, floor_z(y0))]
    wp = cq.Workplane("YZ", origin=(x0 * K, 0, 0))
    return wp.polyline([(y * K, z * K) for y, z in pts]).close().extrude((x1 - x0) * K)


def mirror_x(w):
    return w.mirror("YZ")


# ---------------- channel (front U extension) -----------------
def channel():
    c = 0.29289
    prof = (cq.Workplane("YZ", origin=(-CH_OUT * K, 0, 0))
            .moveTo(0, 0)
            .lineTo((CH_FRONT + CH_R_BOT) * K, 0)
            .threePointArc(((CH_FRONT + CH_R_BOT * c) * K, CH_R_BOT * c * K),
                           (CH_FRONT * K, CH_R_BOT * K))
            .lineTo(CH_FRONT * K, (CH_TOP - CH_R_TOP) * K)
            .threePointArc(((CH_FRONT + CH_R_TOP * c) * K, (CH_TOP - CH_R_TOP * c) * K),
                           ((CH_FRONT + CH_R_TOP) * K, CH_TOP * K))
            .lineTo(0, CH_TOP * K)
            .close()
            .extrude(2 * CH_OUT * K))
    inner = floor_prism(-CH_IN, CH_IN, CH_FRONT - 1, 1)
    ch = prof.cut(inner)
    # small round on the outer edges of the U lip (front outline + wall tops)
    sel = []
    for e in ch.edges().vals():
        bb = e.BoundingBox()
        x0, x1, y1 = bb.xmin / K, bb.xmax / K, bb.ymax / K
        if (abs(abs(x0) - CH_OUT) < 0.05 and abs(abs(x1) - CH_OUT) < 0.05
                and bb.zmin / K > 0.05 and y1 < -0.5):
            sel.append(e)
    if sel:
        try:
            ch = cq.Workplane("XY").add(ch.val().fillet(CH_ROUND * K, sel))
        except Exception:
            pass
    return ch


# ---------------- wall profile with draft ---------------------
def wall_profile(x_in, x_out, z0):
    """XZ outline of a wall/block whose outer face is a large-radius arc:
    vertical at the top edge, curving inward by DRAFT_IN at WALL_BOT."""
    h_ref = TOP_Z - WALL_BOT
    r = (DRAFT_IN ** 2 + h_ref ** 2) / (2.0 * DRAFT_IN)
    cx = x_out - r

    def xat(z):
        return cx + math.sqrt(r * r - (TOP_Z - z) ** 2)

    zm = 0.5 * (z0 + TOP_Z)
    return (x_in, z0), (xat(z0), z0), (xat(zm), zm), (x_out, TOP_Z), (x_in, TOP_Z)


def prism_wall(x_in, x_out, z0, y0, y1, mirror=False):
    p = wall_profile(x_in, x_out, z0)
    s = -1.0 if mirror else 1.0
    pts = [(s * x * K, z * K) for x, z in p]
    wp = (cq.Workplane("XZ", origin=(0, y0 * K, 0))
          .moveTo(*pts[0]).lineTo(*pts[1])
          .threePointArc(pts[2], pts[3])
          .lineTo(*pts[4]).close())
    return wp.extrude(-(y1 - y0) * K)


def side_common():
    # ledge along the inner side of the wall
    s = box(FLOOR_HX, WALL_IN, 0, BODY_Y1, WALL_BOT, LEDGE_TOP)
    # lower rear body (recessed face under the wall overhang)
    s = s.union(box(FLOOR_HX, LOWER_FACE, BOSS_Y0, BODY_Y1, 0, LEDGE_TOP))
    # tall wall (drafted outer face)
    s = s.union(prism_wall(WALL_IN, WALL_OUT, WALL_BOT, 0, BODY_Y1))
    # rear inward lip
    s = s.union(box(FLOOR_HX, WALL_IN, LIP_Y0, BODY_Y1, LEDGE_TOP, TOP_Z))
    # rib on the inner face of the wall
    s = s.union(box(IRIB_IN, WALL_IN, IRIB_Y0, LIP_Y0, LEDGE_TOP, IRIB_Z1))
    # front steps
    s = s.union(box(FLOOR_HX, WALL_IN, 0, STEP1_Y1, LEDGE_TOP, STEP1_Z))
    s = s.union(box(FLOOR_HX, WALL_IN, STEP1_Y1, STEP2_Y1, LEDGE_TOP, STEP2_Z))
    # lower front body
    s = s.union(box(FLOOR_HX, LF_X_HI, 0, LF_Y1, LF_Z, WALL_BOT))
    s = s.union(box(FLOOR_HX, LF_X_LO, 0, LF_Y1, 0, LF_Z))
    # outer rib along the recessed lower face
    s = s.union(box(LOWER_FACE, RIB_OUT, BOSS_Y1, BODY_Y1, RIB_Z0, RIB_Z1))
    return s


def right_side():
    s = side_common()
    # block (drafted outer face)
    s = s.union(prism_wall(WALL_IN, BLK_OUT_R, BLK_BOT_R, 0, BLK_Y1))
    # boss
    s = s.union(box(LF_X_LO, BOSS_X, BOSS_Y0, BOSS_Y1, BOSS_R_Z0, BOSS_R_Z1))
    s = s.cut(cyl_y(BOSS_R_HX, BOSS_R_HZ, BOSS_R, BOSS_Y0 - 1, BOSS_Y1 + 1))
    # blind cross holes
    y, z = XH_UP_R
    s = s.cut(cyl_x(y, z, XH_R, BLK_OUT_R - XH_DEPTH, BLK_OUT_R + 5))
    y, z = XH_LO_R
    s = s.cut(cyl_x(y, z, XH_R, LF_X_HI - XH_LO_DEPTH, LF_X_HI + 1))
    return s


def left_side():
    s = mirror_x(side_common())
    # thickened wall piece below the left block, chamfered at the bottom
    s = s.union(prism_xz([(-WALL_IN, WALL_BOT), (-LW_X + LW_CH, WALL_BOT),
                          (-LW_X, WALL_BOT + LW_CH), (-LW_X, BLK_BOT_L),
                          (-WALL_IN, BLK_BOT_L)], 0, LF_Y1))
    # block
    s = s.union(prism_wall(WALL_IN, BLK_OUT_L, BLK_BOT_L, 0, BLK_Y1, mirror=True))
    # boss (kept below the ledge top on the inside)
    s = s.union(box(-BOSS_X, -WALL_IN, BOSS_Y0, BOSS_Y1, BOSS_L_Z0, BOSS_L_Z1))
    s = s.union(box(-WALL_IN, -LOWER_FACE, BOSS_Y0, BOSS_Y1, BOSS_L_Z0, LEDGE_TOP))
    # lower base on the left
    s = s.union(box(-LB_X, -LF_X_LO, BOSS_Y0, BODY_Y1, 0, LB_Z))
    s = s.cut(cyl_y(BOSS_L_HX, BOSS_L_HZ, BOSS_R, BOSS_Y0 - 1, BOSS_Y1 + 1))
    # counter-bored screw hole through the lower base, slotted at the rear
    s = s.cut(cyl_y(CSK_X, CSK_Z, CSK_R, BOSS_Y0 - 1, BODY_Y1 + 1))
    s = s.cut(cyl_y(CSK_X, CSK_Z, CSK_R2, BOSS_Y0 - 1, BOSS_Y0 + CSK_D))
    cone = cq.Solid.makeCone((CSK_R2 + CSK_CH) * K, CSK_R2 * K, CSK_CH * K,
                             cq.Vector(CSK_X * K, BOSS_Y0 * K, CSK_Z * K), cq.Vector(0, 1, 0))
    s = s.cut(cq.Workplane("XY").add(cone))
    s = s.cut(box(CSK_X, -FLOOR_HX + 1, SLOT_Y0, BODY_Y1 + 1, CSK_Z - CSK_R, CSK_Z + CSK_R))
    # blind cross hole in the left block
    y, z = XH_UP_L
    s = s.cut(cyl_x(y, z, XH_R, -BLK_OUT_L - 5, -BLK_OUT_L + XH_DEPTH))
    return s


body = floor_slab(-FLOOR_HX, FLOOR_HX, 0, FLOOR_Y1)                    # floor plate
body = body.union(box(CH_IN, FLOOR_HX, 0, BRIDGE_Y1, 0, CH_TOP))         # front bridge
body = body.union(box(-FLOOR_HX, -CH_IN, 0, BRIDGE_Y1, 0, CH_TOP))
body = body.union(right_side()).union(left_side())
body = body.union(channel())

# floor holes
for fy in FH_YS:
    body = body.cut(cyl_z(0, fy, FH_R, -5, FLOOR_T + 5))
for sx in (-1, 1):
    body = body.cut(cyl_z(sx * SH_X, SH_Y, SH_R, -5, FLOOR_T + 5))

result = body
